import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.TopExp import TopExp
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE

# =====================================================================
#  Bent lever arm with clevis end and instrument head
#  X : along the straight arm (clevis pin at X=0), Z : up, Y : width
# =====================================================================

# ---------------------------------------------------------------- parameters
TH_DEG = 50.5          # incline of the head leg above horizontal
ARM_H = 34.4           # straight arm height (Z)
ARM_ZC = -1.0          # arm centre height (the clevis is centred on Z=0)
ARM_W = 19.5           # straight arm width (Y)
HEAD_W = 35.5          # head width (Y)
S_TOP = 23.0           # head / inclined leg: upper face offset from the head axis
S_BOT = -21.0          # head / inclined leg: lower face offset from the head axis
TOP_CH = 5.5           # chamfer on the top ridge of the head
P0 = (-290.0, 65.2)    # centre of the head end face (X, Z)
R_IN = 20.0            # inner bend radius
R_OUT = 25.0           # outer bend radius
EDGE_R = 4.0           # edge rounding of the head
ARM_EDGE_R = 7.0       # edge rounding of the straight arm
CH_EDGE_R = 1.5        # rounding along the top chamfer of the head
R_BLEND_X0, R_BLEND_X1 = -252.0, -205.0   # x range where the rounding blends

FORK_ROOT = -66.0      # x where the clevis block starts
FORK_BLK_END = -45.6   # x where the free tines begin (end of gap chamfers)
GAP_BOTTOM = -53.0     # x of the gap bottom between the tines (at its edges)
GAP_FLAT = 14.0        # half width of the gap bottom
GAP_RIDGE = 3.0        # the gap bottom is a shallow ridge along the centre plane
TINE_H = 33.4          # tine height (Z)
TINE_T = 9.5           # tine thickness (Y)
FORK_W = 57.5          # total clevis width (Y)
TINE_R = 4.5           # rounding of the tines
PAD_Z = 16.7           # height of the flat lands at the clevis root

PAD_X0 = -87.5         # start of the flat T-pad on top / bottom of the arm
PAD_XT = -75.0         # start of the full-width part of the pad
PAD_HW = 9.2           # half width of the pad stem
ARM_FORK_W = 33.0      # width of the arm where it meets the clevis

SLOT_X0, SLOT_X1 = -204.0, -108.5   # counterbore extent of the long slot
SLOT_CB_W = 24.0
SLOT_W = 13.4
SLOT_INSET = 5.3
SLOT_CB_D = 4.5

th = math.radians(TH_DEG)
ax = (math.cos(th), -math.sin(th))      # head axis, pointing from the end face into the body
n1 = (math.sin(th), math.cos(th))       # normal of the upper (inner) side of the inclined leg
hT = S_TOP
hf = FORK_W / 2.0
hg = hf - TINE_T
R_T = TINE_H / 2.0


def loc(t, s):
    """head local coords (t along axis from end face, s across) -> (X, Z)"""
    return (P0[0] + t * ax[0] + s * n1[0], P0[1] + t * ax[1] + s * n1[1])


# ---------------------------------------------------------------- side profile (XZ)
zt, zb = ARM_ZC + ARM_H / 2.0, ARM_ZC - ARM_H / 2.0
p_top = loc(0, S_TOP)
inner_corner = loc((p_top[1] - zt) / math.sin(th), S_TOP)
p_bot = loc(0, S_BOT)
outer_corner = loc((p_bot[1] - zb) / math.sin(th), S_BOT)

x_body_end = FORK_ROOT + 6.0
side_pts = [(x_body_end, zt), inner_corner, loc(TOP_CH, S_TOP), loc(0, S_TOP - TOP_CH),
            p_bot, outer_corner, (x_body_end, zb)]
side = (cq.Workplane("XZ").polyline(side_pts).close()
        .extrude(HEAD_W / 2.0 + 5.0, both=True))
side = side.edges("|Y").edges(
    cq.selectors.NearestToPointSelector((inner_corner[0], 0, inner_corner[1]))).fillet(R_IN)
side = side.edges("|Y").edges(
    cq.selectors.NearestToPointSelector((outer_corner[0], 0, outer_corner[1]))).fillet(R_OUT)

# ---------------------------------------------------------------- plan profile (XY)
hw_head, hw_arm, hw_fork = HEAD_W / 2.0, ARM_W / 2.0, ARM_FORK_W / 2.0
xa, xb = -240.0, -201.0     # head -> arm taper
xc, xd = -110.0, -87.0      # arm -> clevis widening
plan = (cq.Workplane("XY").workplane(offset=-60)
        .moveTo(-340, -hw_head)
        .lineTo(xa, -hw_head)
        .spline([(xb, -hw_arm)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
        .lineTo(xc, -hw_arm)
        .spline([(xd, -hw_fork)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
        .lineTo(x_body_end + 5, -hw_fork)
        .lineTo(x_body_end + 5, hw_fork)
        .lineTo(xd, hw_fork)
        .spline([(xc, hw_arm)], tangents=[(-1, 0), (-1, 0)], includeCurrent=True)
        .lineTo(xb, hw_arm)
        .spline([(xa, hw_head)], tangents=[(-1, 0), (-1, 0)], includeCurrent=True)
        .lineTo(-340, hw_head)
        .close()
        .extrude(200))

body = side.intersect(plan)


# variable edge rounding: generous on the straight arm, tighter on the head
def _adjacent_faces(solid):
    emap = TopTools_IndexedDataMapOfShapeListOfShape()
    TopExp.MapShapesAndAncestors_s(solid.wrapped, TopAbs_EDGE, TopAbs_FACE, emap)
    return emap


def _is_smooth(edge, emap):
    faces = [cq.Face(f) for f in emap.FindFromKey(edge.wrapped)]
    if len(faces) != 2:
        return False
    p = edge.positionAt(0.5)
    return abs(faces[0].normalAt(p).dot(faces[1].normalAt(p))) > 0.999


def edge_radius(x):
    if x <= R_BLEND_X0:
        return EDGE_R
    if x >= R_BLEND_X1:
        return ARM_EDGE_R
    return EDGE_R + (ARM_EDGE_R - EDGE_R) * (x - R_BLEND_X0) / (R_BLEND_X1 - R_BLEND_X0)


def round_body(wp):
    solid = wp.val()
    emap = _adjacent_faces(solid)
    mk = BRepFilletAPI_MakeFillet(solid.wrapped)
    for e in wp.edges(cq.selectors.BoxSelector((-400, -100, -100), (x_body_end - 1, 100, 200))).vals():
        if _is_smooth(e, emap):
            continue                      # tangent seams need no rounding
        bb = e.BoundingBox()
        if bb.zmin > zt + 40.0 and bb.xlen < 1.0 and bb.zlen < 1.0:
            mk.Add(CH_EDGE_R, e.wrapped)  # edges of the top chamfer stay crisp
            continue
        mk.Add(edge_radius(e.startPoint().x), edge_radius(e.endPoint().x), e.wrapped)
    mk.Build()
    return cq.Workplane("XY").newObject([cq.Shape.cast(mk.Shape())])


body = round_body(body)


# ---------------------------------------------------------------- local frames on the head
def head_plane(face):
    xd = cq.Vector(ax[0], 0, ax[1])
    if face == "-Y":      # local (x, y) = (t, s)
        return cq.Plane(origin=cq.Vector(P0[0], -HEAD_W / 2.0, P0[1]), xDir=xd,
                        normal=cq.Vector(0, -1, 0))
    if face == "+Y":      # local (x, y) = (t, -s)
        return cq.Plane(origin=cq.Vector(P0[0], HEAD_W / 2.0, P0[1]), xDir=xd,
                        normal=cq.Vector(0, 1, 0))
    if face == "+n1":     # local (x, y) = (t, Y)
        p = loc(0, hT)
        return cq.Plane(origin=cq.Vector(p[0], 0, p[1]), xDir=xd,
                        normal=cq.Vector(n1[0], 0, n1[1]))
    raise ValueError(face)


# ---------------------------------------------------------------- hook bracket under the head
HOOK_W = 25.0
hook_ts = [(7.3, -19.0), (7.3, -22.2), (4.4, -27.4), (5.4, -30.4), (9.0, -32.0),
           (12.9, -33.2), (16.2, -35.9), (15.1, -39.8), (15.0, -43.2), (17.4, -44.5),
           (20.3, -42.7), (21.7, -37.6), (22.0, -33.0), (23.8, -27.5), (34.0, -26.8),
           (46.3, -25.3), (58.7, -23.1), (62.0, -19.0)]
hook = (cq.Workplane("XZ").polyline([loc(t, s) for t, s in hook_ts]).close()
        .extrude(HOOK_W / 2.0, both=True))
hook = hook.edges("|Y").fillet(0.8)
body = body.union(hook)

# ---------------------------------------------------------------- -Y face : pocket, cover plate, flange
POCK_T0, POCK_T1, POCK_S = 4.5, 58.5, 16.8
POCK_SC = 1.0          # pocket centre offset across the head
POCK_D = 3.0
pc_t = (POCK_T0 + POCK_T1) / 2.0
pl = POCK_T1 - POCK_T0


def head_pocket(face):
    wp = cq.Workplane(head_plane(face))
    sc = POCK_SC if face == "-Y" else -POCK_SC
    cut = wp.center(pc_t, sc).rect(pl + 1.6, 2 * POCK_S + 1.6).extrude(-0.8, taper=45)
    cut = cut.union(wp.center(pc_t, sc).rect(pl, 2 * POCK_S).extrude(-POCK_D))
    plate = (cq.Workplane(head_plane(face)).workplane(offset=-POCK_D)
             .center(pc_t, sc).rect(pl - 2.4, 2 * POCK_S - 2.4).extrude(POCK_D - 1.0))
    plate = plate.edges("|Y").fillet(1.2)
    holes = (cq.Workplane(head_plane(face)).workplane(offset=-1.0)
             .pushPoints([(8.5, sc + 12.8), (8.5, sc - 12.8), (54.5, sc + 12.8), (54.5, sc - 12.8)])
             .circle(2.3).extrude(-1.6))
    return cut, plate, holes


for face in ("-Y", "+Y"):
    c, p, h = head_pocket(face)
    body = body.cut(c).union(p).cut(h)

FL_T, FL_R, FL_S = 22.0, 10.5, 0.5
FL_OUT = 3.8
flange = (cq.Workplane(head_plane("-Y")).workplane(offset=-1.0)
          .center(FL_T, FL_S).circle(FL_R).extrude(1.0 + FL_OUT))
flange = flange.faces(cq.selectors.DirectionMinMaxSelector(cq.Vector(0, -1, 0), True)).edges().chamfer(0.6)
body = body.union(flange)
body = body.cut(cq.Workplane(head_plane("-Y")).workplane(offset=FL_OUT)
                .center(FL_T, FL_S).polarArray(8.2, 22.5, 360, 8).circle(1.1).extrude(-2.5))
hub = (cq.Workplane(head_plane("-Y")).workplane(offset=FL_OUT)
       .center(FL_T, FL_S).circle(4.6).extrude(1.4)
       .faces(cq.selectors.DirectionMinMaxSelector(cq.Vector(0, -1, 0), True))
       .workplane().circle(3.0).extrude(2.6))
body = body.union(hub)
body = body.cut(cq.Workplane(head_plane("-Y")).workplane(offset=-1.0)
                .pushPoints([(24.0, 13.0), (33.0, -11.5)]).circle(0.9).extrude(-1.5))

# +Y side : round boss with small screw circle on the cover plate
boss2 = (cq.Workplane(head_plane("+Y")).workplane(offset=-1.0)
         .center(FL_T, -FL_S).circle(8.0).extrude(0.8))
body = body.union(boss2)
body = body.cut(cq.Workplane(head_plane("+Y")).workplane(offset=-0.2)
                .center(FL_T, -FL_S).polarArray(6.0, 0, 360, 6).circle(0.8).extrude(-1.5))

# ---------------------------------------------------------------- +n1 face : screw holes and latch notch
body = body.cut(cq.Workplane(head_plane("+n1"))
                .pushPoints([(24.8, 6.5), (24.8, -6.5), (50.8, 6.5), (50.8, -6.5)])
                .circle(1.5).extrude(-8.0))
NOTCH_T0, NOTCH_T1, NOTCH_Y0, NOTCH_D = 29.0, 42.8, 8.5, 6.0
body = body.cut(cq.Workplane(head_plane("+n1"))
                .center((NOTCH_T0 + NOTCH_T1) / 2.0, (NOTCH_Y0 + HEAD_W / 2.0 + 2.0) / 2.0)
                .rect(NOTCH_T1 - NOTCH_T0, HEAD_W / 2.0 + 2.0 - NOTCH_Y0)
                .extrude(-NOTCH_D))

# ---------------------------------------------------------------- long slot through the arm
slot_c = (SLOT_X0 + SLOT_X1) / 2.0
slot_L = SLOT_X1 - SLOT_X0
body = body.cut(cq.Workplane("XZ").center(slot_c, ARM_ZC)
                .slot2D(slot_L - 2 * SLOT_INSET, SLOT_W).extrude(30, both=True))
for sgn in (1, -1):
    wp = cq.Workplane("XZ").workplane(offset=-sgn * ARM_W / 2.0)   # XZ normal is -Y
    body = body.cut(wp.center(slot_c, ARM_ZC).slot2D(slot_L, SLOT_CB_W).extrude(sgn * SLOT_CB_D))

# ---------------------------------------------------------------- flat T-shaped lands at the clevis root
# the arm is brought to the clevis height in a T shape: a raised land on top,
# a milled land underneath
def t_land(z0, h, bar_hw):
    wp = cq.Workplane("XY").workplane(offset=z0)
    stem = wp.center((PAD_X0 + PAD_XT) / 2.0, 0).rect(PAD_XT - PAD_X0, 2 * PAD_HW).extrude(h)
    bar = (cq.Workplane("XY").workplane(offset=z0)
           .center((PAD_XT + FORK_ROOT + 1.0) / 2.0, 0)
           .rect(FORK_ROOT + 1.0 - PAD_XT, 2 * bar_hw).extrude(h))
    return stem.union(bar)


# full-width block between the flare and the clevis, then the T lands
body = body.union(cq.Workplane("XY").box(FORK_ROOT + 1.0 - PAD_XT, 2 * hw_fork, PAD_Z - zb, centered=False)
                  .translate((PAD_XT, -hw_fork, zb)))
body = body.union(t_land(zt - 2.0, PAD_Z - zt + 2.0, hw_fork))
body = body.cut(t_land(-PAD_Z, -6.0, hw_fork + 2.0))

# ---------------------------------------------------------------- clevis
# sharp block between the tines: ridged gap bottom with chamfers into the tines
block = (cq.Workplane("XY").workplane(offset=-R_T)
         .moveTo(FORK_ROOT, -hg - 0.01).lineTo(FORK_BLK_END, -hg - 0.01)
         .lineTo(GAP_BOTTOM, -GAP_FLAT).lineTo(GAP_BOTTOM + GAP_RIDGE, 0.0)
         .lineTo(GAP_BOTTOM, GAP_FLAT).lineTo(FORK_BLK_END, hg + 0.01).lineTo(FORK_ROOT, hg + 0.01).close()
         .extrude(TINE_H))
fork = block
for sgn in (1, -1):
    y0 = hg if sgn == 1 else -hf
    wp = cq.Workplane("XZ").workplane(offset=-y0)          # plane at Y = y0, normal -Y
    tine = (wp.moveTo(FORK_ROOT, -R_T).lineTo(0, -R_T)
            .threePointArc((R_T, 0), (0, R_T)).lineTo(FORK_ROOT, R_T).close()
            .extrude(-TINE_T))                             # towards +Y
    tine = tine.edges(cq.selectors.BoxSelector((FORK_ROOT + 1.0, -100, -100), (100, 100, 100))).fillet(TINE_R)
    fork = fork.union(tine)

# screw holes on the outer faces of the clevis block and on the arm sides
for sgn in (1, -1):
    wp = cq.Workplane("XZ").workplane(offset=-sgn * hf)
    fork = fork.cut(wp.pushPoints([(-60.3, -10.0), (-60.3, 0.0), (-60.3, 10.0)])
                    .circle(1.7).extrude(sgn * 5.0))
    wp2 = cq.Workplane("XZ").workplane(offset=-sgn * hw_fork)
    body = body.cut(wp2.pushPoints([(-77.0, -7.0), (-77.0, 7.0)]).circle(1.7).extrude(sgn * 5.0))

# bolt circle through the -Y tine
RING_R = 8.2
ring_pts = [(RING_R * math.cos(math.radians(-10 + 45 * k)), RING_R * math.sin(math.radians(-10 + 45 * k)))
            for k in range(8)]
fork = fork.cut(cq.Workplane("XZ").workplane(offset=hf + 1)
                .pushPoints(ring_pts).circle(1.6).extrude(-(TINE_T + 2)))
# recess and centre bore on the inner face of the -Y tine
fork = fork.cut(cq.Workplane("XZ").workplane(offset=hg).circle(11.5).extrude(1.0))
fork = fork.cut(cq.Workplane("XZ").workplane(offset=hg).circle(3.5).extrude(4.0))
# pin head on the inner face of the +Y tine
pin = (cq.Workplane("XZ").workplane(offset=-hg).circle(6.8).extrude(3.8)
       .faces("<Y").edges().chamfer(0.8))
fork = fork.union(pin)

result = body.union(fork)

# split line of the two clevis halves (fine groove on the centre plane)
seam = (cq.Workplane("XY").workplane(offset=-R_T - 1)
        .center((PAD_X0 + GAP_BOTTOM) / 2.0, 0).rect(GAP_BOTTOM - PAD_X0 + 0.6, 0.5)
        .extrude(TINE_H + 2))
core = (cq.Workplane("XY").workplane(offset=-R_T + 0.4)
        .center((PAD_X0 + GAP_BOTTOM) / 2.0 - 0.4, 0).rect(GAP_BOTTOM - PAD_X0 + 0.6, 2.0)
        .extrude(TINE_H - 0.8))
result = result.cut(seam.cut(core))
